import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
LID_AF = 200.0          # lid across flats (regular octagon, flats on X/Y axes)
LID_T = 12.6            # lid plate thickness
LID_CORNER_R = 17.0     # plan-view corner radius of lid
LID_TOP_CHAMFER = 3.0   # chamfered top edge of lid
LID_BOT_FILLET = 0.8

BODY_AF = 188.0         # body across flats
BODY_H = 27.8           # body height (bottom to lid underside)
BODY_CORNER_R = 12.5

TAB_T = 6.0             # mounting ear thickness
TAB_W = 12.5            # mounting ear width
TAB_TIP_C = 108.7       # radius (from part centre) of the ear tip-arc centre; ears point radially
TAB_HOLE_D = 6.0        # keyhole round part
TAB_SLOT_W = 4.0        # keyhole opening to the ear tip
TAB_ROOT_R = 7.0        # blend fillet between ear and the two walls of its corner
TAB_MOUTH_R = 1.5       # rounding of the prong ends at the keyhole mouth

WIN_W = 44.0            # knock-out window width
WIN_Z0 = 5.3            # knock-out bottom height
WIN_DEPTH_TOP = 0.4     # knock-out recess depth at its top
WIN_DEPTH_BOT = 2.0     # knock-out recess depth at its bottom
WIN_R = 5.0             # rounded corners on the front (-Y) knock-out
PULL_W, PULL_H, PULL_D, PULL_Z = 12.0, 7.0, 2.8, 14.3

HOLE_R = 85.0           # radius of lid screw holes (on the vertex directions)
HOLE_D, CSK_D, HOLE_DEPTH = 5.4, 12.5, 3.6   # blind countersunk holes (flat bottom)
CSK_ANGLE = 110.0

EMB_H = 2.0             # height of the embossed logo

TOTAL_H = BODY_H + LID_T


def octagon(af, r, h, z0=0.0):
    """Regular octagon prism with flats on the X/Y axes and rounded vertical corners."""
    circ = (af / 2.0) / math.cos(math.radians(22.5))
    sk = cq.Sketch().regularPolygon(circ, 8, angle=22.5).vertices().fillet(r)
    return cq.Workplane("XY").workplane(offset=z0).placeSketch(sk).extrude(h)


# ---------------- body ----------------
ba = BODY_AF / 2.0
# bottom flange slab: sharp octagon + ears (root blends are filleted on plane/plane edges)
circ_b = ba / math.cos(math.radians(22.5))
flange = cq.Workplane("XY").placeSketch(cq.Sketch().regularPolygon(circ_b, 8, angle=22.5)).extrude(TAB_T)

# ears: one per octagon vertex, pointing radially outward along the vertex direction
ear_angles = [22.5 + 45.0 * k for k in range(8)]
for ang in ear_angles:
    ear = (
        cq.Workplane("XY")
        .center((ba - 5.0 + TAB_TIP_C) / 2.0, 0)
        .rect(TAB_TIP_C - (ba - 5.0), TAB_W)
        .extrude(TAB_T)
        .union(cq.Workplane("XY").center(TAB_TIP_C, 0).circle(TAB_W / 2.0).extrude(TAB_T))
        .rotate((0, 0, 0), (0, 0, 1), ang)
    )
    flange = flange.union(ear)


class RootSel(cq.Selector):
    """Vertical edges where the ears meet the wall (concave root corners)."""

    def __init__(self, rmin, rmax):
        self.rmin, self.rmax = rmin, rmax

    def filter(self, objectList):
        out = []
        for e in objectList:
            if e.geomType() != "LINE":
                continue
            p0, p1 = e.startPoint(), e.endPoint()
            if abs(p0.x - p1.x) > 1e-4 or abs(p0.y - p1.y) > 1e-4:
                continue
            if min(p0.z, p1.z) > 0.05 or abs(max(p0.z, p1.z) - TAB_T) > 0.05:
                continue
            c = e.Center()
            rr = math.hypot(c.x, c.y)
            if self.rmin < rr < self.rmax:
                out.append(e)
        return out


flange = flange.edges(RootSel(90.0, 104.0)).fillet(TAB_ROOT_R)
body = octagon(BODY_AF, BODY_CORNER_R, BODY_H).union(flange)

# keyhole slots in the ears
for ang in ear_angles:
    cutter = (
        cq.Workplane("XY")
        .workplane(offset=-1)
        .center(TAB_TIP_C, 0)
        .circle(TAB_HOLE_D / 2.0)
        .extrude(TAB_T + 2)
        .union(
            cq.Workplane("XY")
            .workplane(offset=-1)
            .center(TAB_TIP_C + 5.0, 0)
            .rect(10.0, TAB_SLOT_W)
            .extrude(TAB_T + 2)
        )
        .rotate((0, 0, 0), (0, 0, 1), ang)
    )
    body = body.cut(cutter)

# rounded prong ends at the keyhole mouths
body = body.edges(RootSel(TAB_TIP_C + 4.0, TAB_TIP_C + TAB_W / 2.0 + 0.5)).fillet(TAB_MOUTH_R)

# knock-out windows with pull tabs on all eight faces.
# The knock-out panel is slightly inclined: shallow at the top, deeper at the bottom.
win_slope = (WIN_DEPTH_BOT - WIN_DEPTH_TOP) / (BODY_H - WIN_Z0)


def win_depth(z):
    return WIN_DEPTH_BOT - (z - WIN_Z0) * win_slope


for k in range(8):
    ang = -90.0 + 45.0 * k          # face normal angle, k=0 -> front (-Y) face
    z1 = BODY_H + 1.0
    prof = [
        (-ba - 6.0, WIN_Z0),
        (-ba + WIN_DEPTH_BOT, WIN_Z0),
        (-ba + win_depth(z1), z1),
        (-ba - 6.0, z1),
    ]
    win = cq.Workplane("YZ").polyline(prof).close().extrude(WIN_W / 2.0, both=True)
    if k == 0:
        win = win.edges("|Y and <Z").fillet(WIN_R)
    y_front = -ba + win_depth(PULL_Z) - PULL_D
    y_back = -ba + WIN_DEPTH_BOT + 0.5
    pull = (
        cq.Workplane("XY")
        .box(PULL_W, y_back - y_front, PULL_H)
        .translate((0, (y_front + y_back) / 2.0, PULL_Z))
    )
    rot = ang + 90.0
    body = body.cut(win.rotate((0, 0, 0), (0, 0, 1), rot))
    body = body.union(pull.rotate((0, 0, 0), (0, 0, 1), rot))

# ---------------- lid ----------------
lid = octagon(LID_AF, LID_CORNER_R, LID_T, BODY_H)
lid = lid.faces(">Z").edges().chamfer(LID_TOP_CHAMFER)
lid = lid.faces("<Z").edges().fillet(LID_BOT_FILLET)

part = body.union(lid)

# countersunk screw holes on the vertex directions
hole_pts = []
for a in (22.5, 157.5, 202.5, 337.5):
    hole_pts.append((HOLE_R * math.cos(math.radians(a)), HOLE_R * math.sin(math.radians(a))))
part = (
    part.faces(">Z").workplane(origin=(0, 0, TOTAL_H))
    .pushPoints(hole_pts)
    .cskHole(HOLE_D, CSK_D, CSK_ANGLE, depth=HOLE_DEPTH)
)

# ---------------- embossed logo ----------------
# triangle stack: (base radius, half width, apex radius)
TRI = [
    (27.2, 11.0, 35.0),
    (35.0, 13.9, 45.5),
    (45.5, 18.7, 59.0),
    (59.0, 24.7, 75.8),
    (75.8, 31.4, 97.0),
]


def tri_solid(base_r, hw, apex_r, ang):
    pts = [(-hw, base_r), (hw, base_r), (0.0, apex_r)]
    t = cq.Workplane("XY").workplane(offset=TOTAL_H - 0.01).polyline(pts).close().extrude(EMB_H + 0.01)
    return t.rotate((0, 0, 0), (0, 0, 1), ang)


emb = None
for ang, n in ((0.0, 5), (180.0, 3), (90.0, 3), (-90.0, 3)):   # +Y, -Y, -X, +X stacks
    for (b, hw, ap) in TRI[:n]:
        t = tri_solid(b, hw, ap, ang)
        emb = t if emb is None else emb.union(t)

Z0 = TOTAL_H - 0.01
EH = EMB_H + 0.01
STROKE = 4.2       # horizontal stroke width of the bold letters
STROKE_V = 3.8     # vertical stroke width


def wp():
    return cq.Workplane("XY").workplane(offset=Z0)


# letter P
P_X0, P_STEM = -25.0, 4.4
P_TOP, P_BOT = 9.6, -9.0
P_BOWL_BOT, P_RIGHT = -3.6, -10.3
pb_r = (P_TOP - P_BOWL_BOT) / 2.0
pb_c = (P_RIGHT - pb_r, (P_TOP + P_BOWL_BOT) / 2.0)
p_stem = wp().center(P_X0 + P_STEM / 2.0, (P_TOP + P_BOT) / 2.0).rect(P_STEM, P_TOP - P_BOT).extrude(EH)
p_bowl_out = (
    wp().center((P_X0 + 1.0 + pb_c[0]) / 2.0, pb_c[1]).rect(pb_c[0] - P_X0 - 1.0, 2 * pb_r).extrude(EH)
    .union(wp().center(*pb_c).circle(pb_r).extrude(EH))
)
p_in_x0 = P_X0 + P_STEM
p_bowl_in = (
    wp().center((p_in_x0 + pb_c[0]) / 2.0, pb_c[1]).rect(pb_c[0] - p_in_x0, 2 * (pb_r - STROKE_V)).extrude(EH)
    .union(wp().center(*pb_c).circle(pb_r - STROKE_V).extrude(EH))
)
letter_p = p_stem.union(p_bowl_out.cut(p_bowl_in))

# letter O with circumflex
o_c = (-0.3, 0.3)
letter_o = wp().center(*o_c).ellipse(8.6, 9.7).extrude(EH).cut(
    wp().center(*o_c).ellipse(8.6 - STROKE, 9.7 - STROKE_V).extrude(EH)
)
circ_pts = [(-4.6, 11.4), (-1.3, 15.4), (1.3, 15.4), (4.6, 11.4), (2.3, 11.4), (0.0, 13.9), (-2.3, 11.4)]
circumflex = wp().polyline(circ_pts).close().extrude(EH)

# letter C
c_c = (17.3, 0.3)
letter_c = (
    wp().center(*c_c).ellipse(7.9, 9.7).extrude(EH)
    .cut(wp().center(*c_c).ellipse(7.9 - STROKE, 9.7 - STROKE_V).extrude(EH))
    .cut(wp().center(c_c[0] + 6.0, c_c[1]).rect(8.0, 7.0).extrude(EH))
)

emb = emb.union(letter_p).union(letter_o).union(circumflex).union(letter_c)

result = part.union(emb)

VIEW = {"azimuth": 45, "elevation": 26}
